import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 120.0          # panel width (X)
L = 67.0           # panel height (Y, in panel plane)
T1 = 1.0           # face plate thickness
T2 = 1.0           # rear pad thickness
R_CORNER = 2.5     # outer corner radius
TILT = 11.2        # panel tilted back about X (deg)

PAD_INSET_X = 2.0  # rear pad inset from outer edge (sides)
PAD_INSET_B = 2.5  # rear pad inset at the lower (front, -Y) edge
PAD_INSET_T = 1.5  # rear pad inset at the upper (+Y) edge
PAD_CHAMFER = 0.8  # bevel on the lower edge of the rear pad
NOTCH = 9.0        # corner notch in rear pad around mount holes
NOTCH_R = 1.5      # inner corner radius of the notch

MH_INSET = 4.25    # mount hole inset from edges
MH_D = 3.0         # mount hole diameter
MH_CB = 5.8        # counterbore diameter
MH_CB_DEPTH = 0.4  # counterbore depth

SLOT_W = 67.4      # display window
SLOT_H = 16.0
SLOT_CY = L / 2 - 13.75

SQ = 19.0          # GEN PUSH square cut-out
SQ_CX = -34.3
ROW_Y = L / 2 - 45.1   # centre line of lower controls

RH_D = 8.9         # round switch holes
RH_X = (11.0, 43.7)

SO_D = 5.5         # display standoffs
SO_H = 3.5
SO_HOLE = 3.0
SO_X_NEG = -44.5   # standoff pair left of window
SO_X_POS = 41.0    # standoff pair right of window
SO_Y = (L / 2 - 10.9, L / 2 - 20.9)

TXT_DEPTH = 0.4
TXT_SIZE = 7.0

# ---------------- face plate ----------------
plate = (
    cq.Workplane("XY")
    .rect(W, L)
    .extrude(-T1)
    .edges("|Z")
    .fillet(R_CORNER)
)

# ---------------- rear pad with corner notches ----------------
pad_len = L - PAD_INSET_B - PAD_INSET_T
pad = (
    cq.Workplane("XY")
    .workplane(offset=-T1)
    .center(0, (PAD_INSET_B - PAD_INSET_T) / 2)
    .rect(W - 2 * PAD_INSET_X, pad_len)
    .extrude(-T2)
    .faces("<Z").edges("<Y")
    .chamfer(PAD_CHAMFER)
)
for sx in (-1, 1):
    for sy in (-1, 1):
        notch = (
            cq.Workplane("XY")
            .workplane(offset=-T1)
            .center(sx * W / 2, sy * L / 2)
            .rect(2 * NOTCH, 2 * NOTCH)
            .extrude(-T2)
            .edges("|Z")
            .fillet(NOTCH_R)
        )
        pad = pad.cut(notch)

body = plate.union(pad)

# ---------------- display standoffs ----------------
so_pts = [(x, y) for x in (SO_X_NEG, SO_X_POS) for y in SO_Y]
standoffs = (
    cq.Workplane("XY")
    .workplane(offset=-T1 - T2)
    .pushPoints(so_pts)
    .circle(SO_D / 2)
    .extrude(-SO_H)
)
body = body.union(standoffs)
so_holes = (
    cq.Workplane("XY")
    .workplane(offset=-T1 - T2 - SO_H)
    .pushPoints(so_pts)
    .circle(SO_HOLE / 2)
    .extrude(SO_H + T2 * 0.5)
)
body = body.cut(so_holes)

# ---------------- through cut-outs ----------------
cut_depth = T1 + T2 + 1
slot = cq.Workplane("XY").workplane(offset=0.5).center(0, SLOT_CY).rect(SLOT_W, SLOT_H).extrude(-cut_depth - 0.5)
square = cq.Workplane("XY").workplane(offset=0.5).center(SQ_CX, ROW_Y).rect(SQ, SQ).extrude(-cut_depth - 0.5)
rounds = (
    cq.Workplane("XY").workplane(offset=0.5)
    .pushPoints([(x, ROW_Y) for x in RH_X])
    .circle(RH_D / 2)
    .extrude(-cut_depth - 0.5)
)
body = body.cut(slot).cut(square).cut(rounds)

# counterbored mount holes (through face plate, inside the pad notches)
mh_pts = [(sx * (W / 2 - MH_INSET), sy * (L / 2 - MH_INSET)) for sx in (-1, 1) for sy in (-1, 1)]
body = body.faces(">Z").workplane().pushPoints(mh_pts).cboreHole(MH_D, MH_CB, MH_CB_DEPTH)

# ---------------- engraved legends ----------------
def legend(txt, x, y, size=TXT_SIZE):
    return (
        cq.Workplane("XY")
        .center(x, y)
        .text(txt, size, -TXT_DEPTH, font="DejaVu Sans", kind="bold", combine=False)
    )

legends = [
    ("GEN PUSH", SQ_CX, L / 2 - 29.9),
    ("FREQ", RH_X[0], L / 2 - 27.0),
    ("SEL", RH_X[0], L / 2 - 35.3),
    ("FREQ", RH_X[1], L / 2 - 27.0),
    ("TGL", RH_X[1], L / 2 - 35.3),
]
for txt, x, y in legends:
    body = body.cut(legend(txt, x, y))

# ---------------- tilt the panel back ----------------
result = body.rotate((0, 0, 0), (1, 0, 0), TILT)
